"""Bracket: round bolting flange with a large bore, a tall curved arm ending
in an eye lug (with gusset "scoop" at its base and a bolt-access pocket), and
a bent fork plate with a U-notch surrounded by 11 holes.

Coordinates: flange centred on the origin, flange bottom at Z=0, arm at -X,
fork at +X, part symmetric about the XZ plane.
"""
import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
# flange (ring) -------------------------------------------------------------
FL_R = 78.0          # flange outer radius
FL_T = 16.0          # flange thickness
BORE_R = 40.0        # central bore radius
CB_R = 51.0          # counterbore radius (underside)
CB_D = 3.0           # counterbore depth
BOLT_R = 68.0        # bolt circle radius
BOLT_D = 7.0         # bolt hole diameter
BOLT_N = 12
BOLT_A0 = 15.0       # first bolt angle (deg)
BOLT_CB = 10.5       # counterbore diameter on the top side
BOLT_CB_D = 3.0      # counterbore depth

# neck / fork plate ---------------------------------------------------------
NECK_W = 70.0        # neck width (Y)
FORK_W = 87.0        # fork plate width (Y)
NECK_FIL = 10.0      # plan fillet between flange and neck
TAPER_X0 = 85.0      # neck starts widening
TAPER_X1 = 119.0     # full fork width reached
BEND_ANG = 63.0      # fork plate inclination (deg from horizontal)
BEND_RU = 53.0       # inner (upper) bend radius
BEND_XU = 72.0       # x where upper bend starts
BEND_RL = 77.5       # outer (lower) bend radius
BEND_XL = 63.0       # x where lower bend starts
FORK_L = 58.3        # straight length of fork plate (outer face)
NOTCH_R = 24.5       # notch radius
NOTCH_S = 37.6       # notch centre along plate (from straight start)
FH_PATH = 34.0       # radius of hole path around the notch
FH_BIG = 11.0        # counterbore dia of the big fork holes (outer face)
FH_CB_D = 6.0        # counterbore depth
FH_SMALL = 5.5       # small fork hole dia

# arm ------------------------------------------------------------------------
ARM_W = 48.0         # arm width (Y)
GUS_ZMAX = 108.0     # top of the gusset body
GUS_D = (-63.0, 28.0)        # gusset side plane: point on flange top (outer)
GUS_C = (-18.0, 50.0)        # gusset side plane: point on flange top (inner)
GUS_A = (-59.4, 24.0, 105.5)  # gusset side plane: point where it meets the arm
ARM_ANG = 63.5       # top segment inclination
GUS_W = 50.0         # half width of the base gusset
ELL_A = 99.4         # gusset elliptic fillet radii
ELL_B = 89.6
ELL_C = (40.0, 105.5)
LUG_R = 29.0         # eye lug radius
LUG_T = 12.0         # eye lug thickness
LUG_CI = (-36.5, 171.8)  # lug centre on the inner face (x, z)
LUG_FLARE = 10.0     # blend radius between lug and arm (in the lug plane)
EYE_R = 16.5         # eye hole radius
EYE_CH = 1.5         # eye hole chamfer
LUG_HOLE_D = 4.0
LUG_HOLE_R = 23.5

# bolt access pocket -------------------------------------------------------
POCK_X = -57.0       # back wall of the bolt access pocket
POCK_W = 56.0        # pocket width (Y)
POCK_FB = 12.0       # floor fillet radius
POCK_WALL = 37.0     # top of the straight back wall
POCK_ARC_MID = (-65.6, 51.9)   # rounded top of the pocket (side profile)
POCK_ARC_END = (-70.4, 61.5)


def xz_plane_wp(w=0.0):
    # workplane in the XZ plane located at Y=+w: local x = global X,
    # local y = global Z, normal = -Y (extrude 2*w for a symmetric body)
    return cq.Workplane(cq.Plane(origin=(0, w, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))


# ---------------------------------------------------------------- base plate
# plan outline: circle + neck with concave fillets
rf = NECK_FIL
hw = NECK_W / 2.0
xf = math.sqrt((FL_R + rf) ** 2 - (hw + rf) ** 2)
tp_c = (xf * FL_R / (FL_R + rf), (hw + rf) * FL_R / (FL_R + rf))  # tangent pt on circle


def fil_mid(sign):
    cx, cy = xf, sign * (hw + rf)
    a1 = math.atan2(tp_c[1] * sign - cy, tp_c[0] - cx)
    a2 = math.atan2(sign * hw - cy, xf - cx)
    am = (a1 + a2) / 2.0
    return (cx + rf * math.cos(am), cy + rf * math.sin(am))


base = cq.Workplane("XY").circle(FL_R).extrude(FL_T)
top_circ = [e for e in base.edges(">Z").vals()
            if e.geomType() == "CIRCLE" and abs(e.radius() - FL_R) < 0.1]
base = base.newObject(top_circ).chamfer(1.0)

# ---------------------------------------------------------------- fork plate
ba = math.radians(BEND_ANG)
ux, uz = math.cos(ba), math.sin(ba)
nx, nz = math.sin(ba), -math.cos(ba)          # outward normal of lower face
pu_end = (BEND_XU + BEND_RU * math.sin(ba), FL_T + BEND_RU * (1 - math.cos(ba)))
pl_end = (BEND_XL + BEND_RL * math.sin(ba), BEND_RL * (1 - math.cos(ba)))
tip_o = (pl_end[0] + FORK_L * ux, pl_end[1] + FORK_L * uz)
# thickness of straight part
FORK_T = (pl_end[0] - pu_end[0]) * nx + (pl_end[1] - pu_end[1]) * nz
tip_i = (tip_o[0] - FORK_T * nx, tip_o[1] - FORK_T * nz)


def arc_mid(cx, cz, r, a0, a1):
    am = (a0 + a1) / 2.0
    return (cx + r * math.cos(am), cz + r * math.sin(am))


# lower arc: centre (BEND_XL, BEND_RL), from angle -90 to -90+BEND_ANG
lm = arc_mid(BEND_XL, BEND_RL, BEND_RL, math.radians(-90), math.radians(-90 + BEND_ANG))
um = arc_mid(BEND_XU, FL_T + BEND_RU, BEND_RU, math.radians(-90), math.radians(-90 + BEND_ANG))

fork_prof = (
    xz_plane_wp(FORK_W / 2.0)
    .moveTo(40, 0)
    .lineTo(BEND_XL, 0)
    .threePointArc(lm, pl_end)
    .lineTo(*tip_o)
    .lineTo(*tip_i)
    .lineTo(*pu_end)
    .threePointArc(um, (BEND_XU, FL_T))
    .lineTo(40, FL_T)
    .close()
    .extrude(FORK_W)
)
# plan limiter: neck width widening to fork width
plan = (
    cq.Workplane("XY").workplane(offset=-5)
    .moveTo(50, -45)
    .lineTo(tp_c[0], -tp_c[1])
    .threePointArc(fil_mid(-1), (xf, -hw))
    .lineTo(TAPER_X0, -hw)
    .spline([(TAPER_X1, -FORK_W / 2)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
    .lineTo(200, -FORK_W / 2)
    .lineTo(200, FORK_W / 2)
    .lineTo(TAPER_X1, FORK_W / 2)
    .spline([(TAPER_X0, hw)], tangents=[(-1, 0), (-1, 0)], includeCurrent=True)
    .lineTo(xf, hw)
    .threePointArc(fil_mid(1), (tp_c[0], tp_c[1]))
    .lineTo(50, 45)
    .close()
    .extrude(150)
)
fork = fork_prof.intersect(plan)

# ---------------------------------------------------------------- arm
aa = math.radians(ARM_ANG)
aux, auz = math.cos(aa), math.sin(aa)
anx, anz = math.sin(aa), -math.cos(aa)        # inner-face normal (points +X/down)
ci = LUG_CI                                    # lug centre on inner face
co = (ci[0] - LUG_T * anx, ci[1] - LUG_T * anz)   # lug centre on outer face
zi = 163.0
p_i163 = (ci[0] - (ci[1] - zi) / math.tan(aa), zi)
zo = 162.0
p_o162 = (co[0] - (co[1] - zo) / math.tan(aa), zo)
ell_left = (ELL_C[0] - ELL_A, ELL_C[1])


# inner (concave) face of arm + gusset: one smooth curve through the measured
# arm points continuing into the elliptic gusset fillet down to the flange
inner_pts = [p_i163, (-50.0, 149.2), (-56.9, 133), (-59.2, 115), ell_left]
for k in range(1, 10):
    th = math.radians(180 + 10 * k)
    inner_pts.append((ELL_C[0] + ELL_A * math.cos(th), ELL_C[1] + ELL_B * math.sin(th)))


def arm_profile(w, s_top=12.0):
    """Side (XZ) profile of arm + gusset extruded symmetrically to +-w.
    s_top: how far the straight top part runs past the lug centre."""
    top_i = (ci[0] + s_top * aux, ci[1] + s_top * auz)
    top_o = (co[0] + s_top * aux, co[1] + s_top * auz)
    return (
        xz_plane_wp(w)
        .moveTo(-69.2, 5)
        .spline([(-69.3, 50), (-68.8, 85), (-66.8, 105), (-64.0, 124), (-61.4, 138),
                 (-58.6, 152), p_o162], tangents=[(0, 1), (aux, auz)], includeCurrent=True)
        .lineTo(*top_o)
        .lineTo(*top_i)
        .spline(inner_pts, tangents=[(-aux, -auz), (1, 0)], includeCurrent=True)
        .lineTo(45, ELL_C[1] - ELL_B)
        .lineTo(45, 5)
        .close()
        .extrude(2 * w)
    )


# constant width arm plate with the eye lug: one side-profile extrusion
# trimmed by the lug outline (circle + tangent flares into the arm width)
lug_c_in = cq.Vector(ci[0], 0, ci[1])
n_in = cq.Vector(anx, 0, anz)
u_arm = cq.Vector(aux, 0, auz)
lug_plane = cq.Plane(origin=lug_c_in, xDir=u_arm, normal=-n_in)   # local y = +Y
wa = ARM_W / 2.0
rfl = LUG_FLARE
fl_s = -math.sqrt((LUG_R + rfl) ** 2 - (wa + rfl) ** 2)
fl_ct = (fl_s * LUG_R / (LUG_R + rfl), (wa + rfl) * LUG_R / (LUG_R + rfl))


def flare_mid(sg):
    a1 = -math.pi / 2 * sg
    a2 = math.atan2(sg * fl_ct[1] - sg * (wa + rfl), fl_ct[0] - fl_s)
    am = (a1 + a2) / 2.0
    return (fl_s + rfl * math.cos(am), sg * (wa + rfl) + rfl * math.sin(am))


lug_outline = (
    cq.Workplane(lug_plane).workplane(offset=-300)
    .moveTo(-400, -wa)
    .lineTo(fl_s, -wa)
    .threePointArc(flare_mid(-1), (fl_ct[0], -fl_ct[1]))
    .threePointArc((LUG_R, 0), (fl_ct[0], fl_ct[1]))
    .threePointArc(flare_mid(1), (fl_s, wa))
    .lineTo(-400, wa)
    .close()
    .extrude(600)
)

# base gusset region: limited in height, with inclined planar side faces that
# fan out from the arm to the flange, and a plan-view cap near the bore
gus_lim = cq.Workplane("XY").workplane(offset=-5).rect(300, 300).extrude(5 + GUS_ZMAX)
for sy in (1, -1):
    D = cq.Vector(GUS_D[0], sy * GUS_D[1], FL_T)
    C = cq.Vector(GUS_C[0], sy * GUS_C[1], FL_T)
    A = cq.Vector(GUS_A[0], sy * GUS_A[1], GUS_A[2])
    nrm = (D - A).cross(C - A).normalized()
    if nrm.y * sy < 0:
        nrm = -nrm
    xd = (C - D).normalized()
    half = (cq.Workplane(cq.Plane(origin=D, xDir=xd, normal=nrm))
            .rect(600, 600).extrude(200))
    gus_lim = gus_lim.cut(half)

plan_pts = [(-70, 30), (-50, 38.5), (-30, 44), (-12, 48.5), (5, 49.5), (20, 47),
            (35, 40), (48, 25), (52, 0), (48, -25), (35, -40), (20, -47), (5, -49.5),
            (-12, -48.5), (-30, -44), (-50, -38.5), (-70, -30)]
gus_plan = (
    cq.Workplane("XY").workplane(offset=-5)
    .moveTo(-90, -28)
    .lineTo(-90, 28)
    .lineTo(-80, 28)
    .spline(plan_pts + [(-80, -28)], includeCurrent=True)
    .close()
    .extrude(260)
)
gus_lim = gus_lim.intersect(gus_plan)

# arm + lug + gusset = one side-profile extrusion trimmed by the width limiters
arm = arm_profile(GUS_W, s_top=LUG_R + 8).intersect(lug_outline.union(gus_lim))

# ---------------------------------------------------------------- union
body = base.union(fork).union(arm)

# ---------------------------------------------------------------- cuts
# central bore (limited height so the lug stays intact)
bore = cq.Workplane("XY").workplane(offset=-1).circle(BORE_R).extrude(125)
body = body.cut(bore)
cbore = cq.Workplane("XY").workplane(offset=-1).circle(CB_R).extrude(1 + CB_D)
body = body.cut(cbore)

# bolt holes
bolt_pts = [(BOLT_R * math.cos(math.radians(BOLT_A0 + i * 360.0 / BOLT_N)),
             BOLT_R * math.sin(math.radians(BOLT_A0 + i * 360.0 / BOLT_N))) for i in range(BOLT_N)]
bolts = (cq.Workplane("XY").workplane(offset=-1).pushPoints(bolt_pts)
         .circle(BOLT_D / 2).extrude(FL_T + 2))
body = body.cut(bolts)
# counterbore on the top side of every bolt hole
cbs = (cq.Workplane("XY").workplane(offset=FL_T - BOLT_CB_D).pushPoints(bolt_pts)
       .circle(BOLT_CB / 2).extrude(BOLT_CB_D + 1))
body = body.cut(cbs)

# bolt-access pocket at the outer base of the arm
c45 = math.cos(math.radians(45))
pocket = (
    xz_plane_wp(POCK_W / 2)
    .moveTo(-95, FL_T)
    .lineTo(POCK_X - POCK_FB, FL_T)
    .threePointArc((POCK_X - POCK_FB + POCK_FB * c45, FL_T + POCK_FB - POCK_FB * c45),
                   (POCK_X, FL_T + POCK_FB))
    .lineTo(POCK_X, POCK_WALL)
    .threePointArc(POCK_ARC_MID, POCK_ARC_END)
    .lineTo(-95, POCK_ARC_END[1])
    .close()
    .extrude(POCK_W)
)
body = body.cut(pocket)

# eye hole + small holes on outer face
eye = cq.Workplane(lug_plane).workplane(offset=-5).circle(EYE_R).extrude(LUG_T + 10)
body = body.cut(eye)
for (org, dirv) in ((lug_c_in, -n_in), (lug_c_in - n_in * LUG_T, n_in)):
    # 45 deg chamfer cone at both ends of the eye hole (dirv points into the lug)
    r_face = EYE_R + EYE_CH
    cone = cq.Solid.makeCone(r_face + 2.0, 0.0, r_face + 2.0,
                             pnt=org - dirv * 2.0, dir=dirv)
    body = body.cut(cq.Workplane("XY").add(cone))
lug_out_plane = cq.Plane(origin=lug_c_in + (-n_in) * LUG_T, xDir=u_arm, normal=n_in)
small = (cq.Workplane(lug_out_plane)
         .pushPoints([(LUG_HOLE_R, 0), (0, LUG_HOLE_R), (0, -LUG_HOLE_R)])
         .circle(LUG_HOLE_D / 2).extrude(8))
body = body.cut(small)

# fork notch + holes (plate frame on the lower / outer face)
p0 = cq.Vector(pl_end[0], 0, pl_end[1])
u_f = cq.Vector(ux, 0, uz)
n_f = cq.Vector(nx, 0, nz)
pc = p0 + u_f * NOTCH_S
fork_plane = cq.Plane(origin=pc - n_f * (FORK_T + 5), xDir=u_f, normal=n_f)
notch = (cq.Workplane(fork_plane).circle(NOTCH_R).extrude(FORK_T + 10)
         .union(cq.Workplane(fork_plane).center(30, 0).rect(60, 2 * NOTCH_R).extrude(FORK_T + 10)))
body = body.cut(notch)

big_pts, small_pts = [], []
for k in range(9):
    al = math.radians(22.5 * k)
    p = (-FH_PATH * math.sin(al), FH_PATH * math.cos(al))
    (big_pts if k % 2 == 0 else small_pts).append(p)
small_pts += [(13.0, FH_PATH), (13.0, -FH_PATH)]
# all 11 holes go through with the small diameter ...
fh = (cq.Workplane(fork_plane).pushPoints(big_pts + small_pts)
      .circle(FH_SMALL / 2).extrude(FORK_T + 10))
body = body.cut(fh)
# ... and every second one is counterbored from the outer (lower) face
fork_out_plane = cq.Plane(origin=pc + n_f * 2.0, xDir=u_f, normal=-n_f)
fcb = (cq.Workplane(fork_out_plane).pushPoints(big_pts)
       .circle(FH_BIG / 2).extrude(2.0 + FH_CB_D))
body = body.cut(fcb)

# fully rounded prong tips (semicircular ends across the prong width)
tip_s = FORK_L - NOTCH_S
hwf = FORK_W / 2.0
r_t = (hwf - NOTCH_R) / 2.0
y_t = (hwf + NOTCH_R) / 2.0
for sy in (1, -1):
    box = (cq.Workplane(fork_plane).center(tip_s - r_t / 2 + 2.5, sy * y_t)
           .rect(r_t + 5, 2 * r_t + 4).extrude(FORK_T + 10))
    cyl = cq.Workplane(fork_plane).center(tip_s - r_t, sy * y_t).circle(r_t).extrude(FORK_T + 10)
    body = body.cut(box.cut(cyl))

result = body
